import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FRAME_AF = 100.0      # outer thin hex frame, across flats
FRAME_W = 0.25        # frame band width
FRAME_H = 0.25        # frame height

PLATE_AF = 80.0       # hex plate across flats (vertices on +/-Y)
T_TOP = 0.6           # upper (full outline) layer thickness
T_BOT = 0.6           # lower (inset) layer thickness
BOT_INSET = 3.0       # inset of lower layer from plate outline
T = T_TOP + T_BOT

# bayonet notches on the two lower edges
NOTCH_X = 31.75       # |x| of notch centre on the edge
NOTCH_W = 4.5         # notch width (perpendicular to its walls)
NOTCH_D_TOP = 4.5     # notch depth in upper layer
NOTCH_ANG = 45.0      # wall direction (deg from -Y axis)

# threaded collar on top of the plate
RING_R_IN = 24.2      # bore radius of collar
RING_R_ROOT = 25.0    # thread root / tube outer radius
RING_R_CREST = 26.9   # thread crest radius
RING_H = 3.5          # collar height above plate top
THREAD_P = 3.2        # thread pitch
THREAD_Z0 = 2.3       # crest height above plate at +X
THREAD_HW_ROOT = 1.3  # half width of thread at root
THREAD_HW_CREST = 0.25 # half width of flat at thread crest
THREAD_LEAD_R = 26.2   # thread radius at top after lead-in chamfer
DISK_DEPTH = 0.35     # recess of the disk inside the collar
BORE_CREASE = 0.35    # height of draft break on the bore wall
BORE_CHAMFER = 0.7    # radial size of steep chamfer on inner top edge of collar
BORE_CHAMFER_H = 1.4  # axial size of that chamfer

# hexagonal groove on top (vertices on +/-X, stretched towards +Y)
GRV_Y0 = -0.6         # y of the two side vertices
GRV_OUT_VX = 37.7     # outer outline: side vertex x
GRV_OUT_TOP = 36.5    # outer outline: top edge y
GRV_OUT_BOT = -33.9   # outer outline: bottom edge y
GRV_IN_VX = 34.7      # inner outline: side vertex x
GRV_IN_TOP = 33.8     # inner outline: top edge y
GRV_IN_BOT = -31.2    # inner outline: bottom edge y
GRV_IN_CLIP = 4.7     # inset of plate edge that clips inner outline corners
GRV_DEPTH = 0.5

# underside: three rails on alternate edges, three skewed label pads
RAIL_DIST = 33.0      # rail centre distance from plate centre
RAIL_LEN = 41.0
RAIL_W = 2.2
RAIL_DEPTH = 0.25
PAD_DEPTH = 0.1


def hex_pts(af, rot=90.0):
    r = af / math.sqrt(3.0)
    return [(r * math.cos(math.radians(rot + 60 * i)),
             r * math.sin(math.radians(rot + 60 * i))) for i in range(6)]


def prism(pts, z0, h):
    return cq.Workplane("XY").workplane(offset=z0).polyline(pts).close().extrude(h)


# ---------------- outer thin frame ----------------
frame = (prism(hex_pts(FRAME_AF), 0, FRAME_H)
         .cut(prism(hex_pts(FRAME_AF - 2 * FRAME_W), -1, FRAME_H + 2)))

# ---------------- plate ----------------
top_layer = prism(hex_pts(PLATE_AF), T_BOT, T_TOP)
bot_layer = prism(hex_pts(PLATE_AF - 2 * BOT_INSET), 0, T_BOT + 0.01)
plate = top_layer.union(bot_layer)


def notch_cut(sign, depth, z0, h):
    """Notch polygon: walls along NOTCH_ANG, inner end wall parallel to edge."""
    R = PLATE_AF / math.sqrt(3.0)
    x = sign * NOTCH_X
    y = -R + abs(x) * math.tan(math.radians(30))     # point on the lower edge
    a = math.radians(90 + sign * NOTCH_ANG)
    d = (math.cos(a), math.sin(a))                    # into the plate
    n = (-d[1], d[0])
    en = (-0.5 * sign, math.sqrt(3) / 2)              # edge inward normal
    dn = d[0] * en[0] + d[1] * en[1]
    nn = n[0] * en[0] + n[1] * en[1]
    w = NOTCH_W / 2
    back = 3.0                                        # overshoot outside the edge
    pts = []
    for t in (-w, w):
        s_in = (depth - t * nn) / dn
        pts.append((x + n[0] * t + d[0] * s_in, y + n[1] * t + d[1] * s_in))
    pts = [(x - n[0] * w - d[0] * back, y - n[1] * w - d[1] * back), pts[0], pts[1],
           (x + n[0] * w - d[0] * back, y + n[1] * w - d[1] * back)]
    return prism(pts, z0, h)


for sgn in (-1, 1):
    plate = plate.cut(notch_cut(sgn, NOTCH_D_TOP, T_BOT - 0.01, T_TOP + 1))

# ---------------- hexagonal groove on top ----------------


def grv_poly(vx, top, bot):
    k = math.tan(math.radians(60))
    xt = vx - (top - GRV_Y0) / k
    xb = vx - (GRV_Y0 - bot) / k
    return [(vx, GRV_Y0), (xt, top), (-xt, top), (-vx, GRV_Y0), (-xb, bot), (xb, bot)]


def plate_clip(inset, z0, h):
    return prism(hex_pts(PLATE_AF - 2 * inset), z0, h)


g_out = prism(grv_poly(GRV_OUT_VX, GRV_OUT_TOP, GRV_OUT_BOT), T - GRV_DEPTH, 1)
g_out = g_out.intersect(plate_clip(0.25, T - GRV_DEPTH, 1))
g_in = prism(grv_poly(GRV_IN_VX, GRV_IN_TOP, GRV_IN_BOT), T - GRV_DEPTH - 1, 3)
g_in = g_in.intersect(plate_clip(GRV_IN_CLIP, T - GRV_DEPTH - 1, 3))
groove = g_out.cut(g_in)
plate = plate.cut(groove)

# ---------------- threaded collar ----------------
# thin tube with a single-start external thread (right hand)
core_prof = [
    (RING_R_IN - 0.2, -DISK_DEPTH),
    (RING_R_IN, BORE_CREASE),
    (RING_R_IN, RING_H),
    (RING_R_ROOT, RING_H),
    (RING_R_ROOT, -DISK_DEPTH),
]
core = (cq.Workplane("XZ").polyline([(r, z + T) for r, z in core_prof]).close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), 225))   # park the revolve seam edge-on

z0 = T + THREAD_Z0 - 2 * THREAD_P
helix = cq.Wire.makeHelix(pitch=THREAD_P, height=3 * THREAD_P,
                          radius=RING_R_ROOT - 0.2, center=cq.Vector(0, 0, z0))
r_sh = RING_R_CREST - 0.35          # shoulder where the rounded crest starts
hw_sh = THREAD_HW_CREST + 0.3
thread = (cq.Workplane("XZ")
          .moveTo(RING_R_ROOT - 0.2, z0 - THREAD_HW_ROOT)
          .lineTo(r_sh, z0 - hw_sh)
          .threePointArc((RING_R_CREST, z0), (r_sh, z0 + hw_sh))
          .lineTo(RING_R_ROOT - 0.2, z0 + THREAD_HW_ROOT)
          .close()
          .sweep(cq.Workplane().add(helix), isFrenet=True))
# envelope with a 45 deg lead-in chamfer at the top of the thread
env_prof = [(0, T - 0.01), (RING_R_CREST + 1, T - 0.01),
            (RING_R_CREST + 1, T + RING_H - (RING_R_CREST + 1 - THREAD_LEAD_R)),
            (THREAD_LEAD_R, T + RING_H), (0, T + RING_H)]
env = (cq.Workplane("XZ").polyline(env_prof).close()
       .revolve(360, (0, 0, 0), (0, 1, 0)))
thread = thread.intersect(env)

# recessed disk inside the collar
disk = (cq.Workplane("XY").workplane(offset=T - DISK_DEPTH)
        .circle(RING_R_IN - 0.1).extrude(DISK_DEPTH + 1))
plate = plate.cut(disk).union(core).union(thread)

# steep chamfer on the inner top edge of the collar (cuts tube and thread)
k = BORE_CHAMFER_H / BORE_CHAMFER
ch_prof = [(RING_R_IN - 0.5, T + RING_H - BORE_CHAMFER_H - 0.5 * k),
           (RING_R_IN + BORE_CHAMFER + 0.5 / k, T + RING_H + 0.5),
           (RING_R_IN - 0.5, T + RING_H + 0.5)]
ch_cut = (cq.Workplane("XZ").polyline(ch_prof).close()
          .revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), 225))
plate = plate.cut(ch_cut)

# ---------------- underside features ----------------
for ang in (-60.0, 180.0, 60.0):
    a = math.radians(ang)
    cx, cy = RAIL_DIST * math.cos(a), RAIL_DIST * math.sin(a)
    slot = (cq.Workplane("XY").center(cx, cy)
            .slot2D(RAIL_LEN, RAIL_W, ang + 90).extrude(RAIL_DEPTH))
    plate = plate.cut(slot)

pads = [
    [(10.3, -23.4), (22.2, -23.4), (-11.3, 25.7), (-23.2, 25.7)],
    [(-12.9, -23.4), (-0.3, -23.4), (-17.2, 0.9), (-29.3, 0.9)],
    [(15.2, 1.7), (28.15, 1.7), (11.8, 25.3), (-0.6, 25.3)],
]
for p in pads:
    plate = plate.cut(prism(p, -1, 1 + PAD_DEPTH))

# ---------------- engraved rotation glyphs (underside) ----------------


def circle3(p1, p2, p3):
    ax, ay = p1
    bx, by = p2
    cx_, cy_ = p3
    d = 2 * (ax * (by - cy_) + bx * (cy_ - ay) + cx_ * (ay - by))
    ux = ((ax ** 2 + ay ** 2) * (by - cy_) + (bx ** 2 + by ** 2) * (cy_ - ay)
          + (cx_ ** 2 + cy_ ** 2) * (ay - by)) / d
    uy = ((ax ** 2 + ay ** 2) * (cx_ - bx) + (bx ** 2 + by ** 2) * (ax - cx_)
          + (cx_ ** 2 + cy_ ** 2) * (bx - ax)) / d
    return ux, uy, math.hypot(ax - ux, ay - uy)


def arc_stroke(cx, cy, rho, w, a0, a1, depth, head=True):
    """Engraved arc of radius rho (deg a0 -> a1) with optional arrow head at a1."""
    def pol(r, a):
        return (cx + r * math.cos(math.radians(a)), cy + r * math.sin(math.radians(a)))
    am = 0.5 * (a0 + a1)
    ro, ri = rho + w / 2, rho - w / 2
    sk = (cq.Workplane("XY").workplane(offset=-1)
          .moveTo(*pol(ro, a0)).threePointArc(pol(ro, am), pol(ro, a1))
          .lineTo(*pol(ri, a1)).threePointArc(pol(ri, am), pol(ri, a0)).close()
          .extrude(1 + depth))
    if head:
        sgn = 1 if a1 > a0 else -1
        tip_a = a1 + sgn * math.degrees(1.6 * w / rho)
        tri = [pol(rho + 1.4 * w, a1), pol(rho - 1.4 * w, a1), pol(rho, tip_a)]
        sk = sk.union(prism(tri, -1, 1 + depth))
    return sk


GLYPH_D = 0.12
GLYPH_W = 0.5
# left glyph: curved arrow with short hooked stroke
ux, uy, ur = circle3((-24.4, -25.9), (-28.1, -21.9), (-29.2, -16.6))


def ang(p):
    return math.degrees(math.atan2(p[1] - uy, p[0] - ux)) % 360.0


a_s, a_m, a_e = ang((-24.4, -25.9)), ang((-28.1, -21.9)), ang((-29.2, -16.6))
if (a_m - a_s) % 360.0 < (a_e - a_s) % 360.0:      # counter-clockwise through mid
    a_e = a_s + (a_e - a_s) % 360.0
else:                                              # clockwise through mid
    a_e = a_s - (a_s - a_e) % 360.0
plate = plate.cut(arc_stroke(ux, uy, ur, GLYPH_W, a_s, a_e, GLYPH_D))
plate = plate.cut(arc_stroke(-23.0, -21.6, 2.2, GLYPH_W, 185.0, 115.0, GLYPH_D, head=False))
plate = plate.cut(cq.Workplane("XY").workplane(offset=-1).center(-24.0, -18.3)
                  .circle(0.55).extrude(1 + GLYPH_D))
# right glyph: small ring with curved arrow around it
plate = plate.cut(cq.Workplane("XY").workplane(offset=-1).center(29.25, 11.35)
                  .circle(2.3).circle(1.3).extrude(1 + GLYPH_D))
plate = plate.cut(arc_stroke(29.25, 11.35, 4.4, GLYPH_W, -50.0, 95.0, GLYPH_D))

result = plate.union(frame)
